import math
import cadquery as cq

# =====================================================================
#  Cylindrical housing with a front window bore and a screwed rear cap
#  Axis of the part = global X.  Front face (+X) carries a shallow
#  recess, a deep window bore and four socket head cap screws; the rear
#  (-X) face carries a filleted boss closed by a cap held by four
#  counterbored screws, plus two plain holes.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
BODY_D = 120.0          # main housing diameter
BODY_L = 52.3           # main housing length (along X)

FRONT_STEP_D = 100.2    # shallow recess diameter on the front face
FRONT_STEP_DEPTH = 2.5  # shallow recess depth
BORE_D = 83.4           # window bore diameter
BORE_DEPTH = 10.3       # bore depth measured from the shallow recess floor

BOSS_D = 94.3           # rear boss diameter
BOSS_L = 9.45           # rear boss length
BOSS_FILLET = 3.5       # fillet at the boss root
CAP_D = 94.1            # rear cap diameter (slightly under boss -> seam line)
CAP_L = 10.6            # rear cap length
CAP_CHAMFER = 0.4       # chamfer on the cap end face

# front socket head cap screws (4 at 0/90/180/270 deg)
F_SCREW_R = 55.8        # pitch radius
F_HEAD_D = 7.2
F_HEAD_H = 4.6
F_HEAD_CHAMFER = 0.0     # top edge of the heads left sharp
F_HEX_AF = 3.2          # hex socket across flats
F_HEX_DEPTH = 2.4

# rear cap screws (4 at 45 deg positions) in counterbores + 2 plain holes
R_PITCH_R = 40.0
R_CBORE_D = 8.0
R_CBORE_DEPTH = 4.5
R_HEAD_D = 7.0
R_HEAD_RECESS = 0.3
R_HEX_AF = 3.0
R_HEX_DEPTH = 2.0
R_HOLE_D = 5.0          # plain holes: counterbore diameter
R_HOLE_CB_DEPTH = 2.5   #   counterbore depth
R_HOLE_D2 = 3.0         #   tapping hole diameter
R_HOLE_DEPTH = 8.0      #   total depth

# angular position of the revolve seams (cosmetic: keep them out of sight)
OUTER_SEAM_DEG = -60.0
INNER_SEAM_DEG = 145.0


# ---------------- helpers ----------------
def yz_point(r, ang_deg):
    """point on a circle of radius r in the YZ plane, returned as (y, z)"""
    a = math.radians(ang_deg)
    return (r * math.cos(a), r * math.sin(a))


def revolve_x(pts_builder, seam_deg):
    """revolve an (x, r) profile drawn in XY about the X axis"""
    solid = pts_builder.revolve(360, (0, 0, 0), (1, 0, 0))
    return solid.rotate((0, 0, 0), (1, 0, 0), seam_deg)


def hex_socket(x0, r, angles, af, depth, direction):
    """hexagonal socket prisms on a bolt circle starting at plane x0 and
    going along +/-X; like a polar pattern, each hex has a corner pointing
    along its own radial direction"""
    d_corner = af / math.cos(math.pi / 6)
    prisms = None
    for a in angles:
        y, z = yz_point(r, a)
        p = (cq.Workplane("YZ").workplane(offset=x0)
             .center(y, z).polygon(6, d_corner)
             .extrude(depth * direction)
             .rotate((x0, y, z), (x0 + 1, y, z), a))
        prisms = p if prisms is None else prisms.union(p)
    return prisms


# ---------------- main housing (revolved profiles) ----------------
x_back = -BOSS_L - CAP_L
R_body, R_boss, R_cap = BODY_D / 2, BOSS_D / 2, CAP_D / 2
R_step, R_bore = FRONT_STEP_D / 2, BORE_D / 2
f = BOSS_FILLET
c45 = math.cos(math.radians(45))

outer_profile = (cq.Workplane("XY")
                 .moveTo(x_back, 0)
                 .lineTo(x_back, R_cap - CAP_CHAMFER)
                 .lineTo(x_back + CAP_CHAMFER, R_cap)
                 .lineTo(-BOSS_L, R_cap)
                 .lineTo(-BOSS_L, R_boss)
                 .lineTo(-f, R_boss)
                 .threePointArc((-f + f * c45, R_boss + f - f * c45), (0, R_boss + f))
                 .lineTo(0, R_body)
                 .lineTo(BODY_L, R_body)
                 .lineTo(BODY_L, 0)
                 .close())
housing = revolve_x(outer_profile, OUTER_SEAM_DEG)

# front shallow recess + window bore, cut as one revolved tool
x_step = BODY_L - FRONT_STEP_DEPTH
x_floor = x_step - BORE_DEPTH
inner_profile = (cq.Workplane("XY")
                 .moveTo(x_floor, 0)
                 .lineTo(x_floor, R_bore)
                 .lineTo(x_step, R_bore)
                 .lineTo(x_step, R_step)
                 .lineTo(BODY_L + 1.0, R_step)
                 .lineTo(BODY_L + 1.0, 0)
                 .close())
housing = housing.cut(revolve_x(inner_profile, INNER_SEAM_DEG))

# ---------------- front socket head cap screws ----------------
front_ang = (0, 90, 180, 270)
front_pts = [yz_point(F_SCREW_R, a) for a in front_ang]
heads = (cq.Workplane("YZ").workplane(offset=BODY_L)
         .pushPoints(front_pts).circle(F_HEAD_D / 2).extrude(F_HEAD_H))
if F_HEAD_CHAMFER > 0:
    heads = heads.faces(">X").edges().chamfer(F_HEAD_CHAMFER)
heads = heads.cut(hex_socket(BODY_L + F_HEAD_H + 0.5, F_SCREW_R, front_ang,
                             F_HEX_AF, F_HEX_DEPTH + 0.5, -1))
housing = housing.union(heads)

# ---------------- rear cap: counterbored screws and plain holes ----------------
rear_ang = (45, 135, 225, 315)
rear_scr = [yz_point(R_PITCH_R, a) for a in rear_ang]
rear_holes = [yz_point(R_PITCH_R, a) for a in (90, 270)]

cbores = (cq.Workplane("YZ").workplane(offset=x_back)
          .pushPoints(rear_scr).circle(R_CBORE_D / 2).extrude(R_CBORE_DEPTH))
housing = housing.cut(cbores)

rheads = (cq.Workplane("YZ").workplane(offset=x_back + R_HEAD_RECESS)
          .pushPoints(rear_scr).circle(R_HEAD_D / 2)
          .extrude(R_CBORE_DEPTH - R_HEAD_RECESS + 0.01))
rheads = rheads.cut(hex_socket(x_back + R_HEAD_RECESS - 0.5, R_PITCH_R, rear_ang,
                               R_HEX_AF, R_HEX_DEPTH + 0.5, 1))
housing = housing.union(rheads)

holes = (cq.Workplane("YZ").workplane(offset=x_back - 1)
         .pushPoints(rear_holes).circle(R_HOLE_D / 2).extrude(R_HOLE_CB_DEPTH + 1))
holes = holes.union(cq.Workplane("YZ").workplane(offset=x_back - 1)
                    .pushPoints(rear_holes).circle(R_HOLE_D2 / 2)
                    .extrude(R_HOLE_DEPTH + 1))
housing = housing.cut(holes)

result = housing

VIEW = {"azimuth": 45, "elevation": 26}
